import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 21            # tooth count
R_TIP = 30.0            # outside (tip) radius
R_ROOT = 24.18          # root radius
TOOTH_HALF_W = 2.25     # half width of a tooth at the root circle
TIP_HALF_W = 0.89       # half width of the flat tip land
FLANK_RADIUS = 8.05     # radius of the convex (arc) tooth flank
THICK = 7.2              # plate thickness (along Y)

R_RIM_IN = 21.5         # inner radius of the rim (outer edge of the windows)
N_SPOKES = 3            # number of curved spokes / windows
LENS_OFFSET = 24.94     # distance from axis to centre of the window arc
LENS_R = 20.31           # radius of the window's inner arc
R_HUB = 5.03            # hub radius (clips the window tips)
R_HOLE = 3.18           # bore radius
HUB_BLEND = 0.8         # fillet blending the hub boss into the window arcs

TOOTH_PHASE = 0.0       # angle of first tooth from +X (deg)
WINDOW_PHASE = 90.0     # first window centred straight up (+Z)

VIEW = {"azimuth": 45, "elevation": 26}


def _gear_outline_segs():
    """Segments (kind, p0, pmid, p1) describing the outer gear outline in 2D."""
    pitch = 2 * math.pi / N_TEETH
    w0 = TOOTH_HALF_W
    vb = math.sqrt(R_ROOT ** 2 - w0 ** 2)          # flank foot on root circle
    wt = TIP_HALF_W
    vt = math.sqrt(R_TIP ** 2 - wt ** 2)           # land corner on tip circle
    # single convex flank arc of radius FLANK_RADIUS from foot to land corner
    cw, cv = 0.5 * (w0 + wt), 0.5 * (vb + vt)
    chord = math.hypot(wt - w0, vt - vb)
    sag = FLANK_RADIUS - math.sqrt(FLANK_RADIUS ** 2 - (0.5 * chord) ** 2)
    nx, ny = (vt - vb) / chord, -(wt - w0) / chord  # outward normal of chord
    M = (cw + sag * nx, cv + sag * ny)
    delta = math.atan2(w0, vb)

    def g(pt, th):
        w, v = pt
        return (w * math.sin(th) + v * math.cos(th),
                -w * math.cos(th) + v * math.sin(th))

    segs = []
    for k in range(N_TEETH):
        th = math.radians(TOOTH_PHASE) + k * pitch
        segs.append(("arc", g((w0, vb), th), g(M, th), g((wt, vt), th)))
        segs.append(("arc", g((wt, vt), th), g((0.0, R_TIP), th), g((-wt, vt), th)))
        segs.append(("arc", g((-wt, vt), th), g((-M[0], M[1]), th), g((-w0, vb), th)))
        a0 = th + delta
        a1 = th + pitch - delta
        am = th + 0.5 * pitch
        segs.append(("arc", (R_ROOT * math.cos(a0), R_ROOT * math.sin(a0)),
                     (R_ROOT * math.cos(am), R_ROOT * math.sin(am)),
                     (R_ROOT * math.cos(a1), R_ROOT * math.sin(a1))))
    return segs


def _wp(depth):
    """XZ workplane placed so that extruding `depth` is centred on Y = 0."""
    return cq.Workplane("XZ", origin=(0, depth / 2.0, 0))


def make_gear_blank():
    segs = _gear_outline_segs()
    wp = _wp(THICK).moveTo(*segs[0][1])
    for kind, p0, pm, p1 in segs:
        if kind == "line":
            wp = wp.lineTo(*p1)
        else:
            wp = wp.threePointArc(pm, p1)
    return wp.close().extrude(THICK)


def _cyl(r, cx=0.0, cz=0.0, depth=None):
    depth = THICK * 2.0 if depth is None else depth
    return _wp(depth).center(cx, cz).circle(r).extrude(depth)


def make_window(phi_deg):
    """Lens shaped window: inside the rim, inside the offset arc, outside the hub."""
    phi = math.radians(phi_deg)
    cx, cz = LENS_OFFSET * math.cos(phi), LENS_OFFSET * math.sin(phi)
    return _cyl(R_RIM_IN).intersect(_cyl(LENS_R, cx, cz)).cut(_cyl(R_HUB, depth=THICK * 3))


gear = make_gear_blank()
for i in range(N_SPOKES):
    gear = gear.cut(make_window(WINDOW_PHASE + i * 360.0 / N_SPOKES))

gear = gear.cut(_cyl(R_HOLE))

# soften the notches where the hub boss meets the curved window arcs
_solid = gear.val()
_hub_edges = [
    e for e in _solid.Edges()
    if e.geomType() == "LINE"
    and abs(math.hypot(e.startPoint().x, e.startPoint().z) - R_HUB) < 1e-3
]
if HUB_BLEND > 0 and _hub_edges:
    gear = cq.Workplane("XY").newObject([_solid.fillet(HUB_BLEND, _hub_edges)])

result = gear
